import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 146.7          # length along X
D = 90.0           # depth along Y (front face at -Y)
H = 60.0           # height along Z

R_BACK = 5.5       # fillet on the two long back edges (+Y, +-Z)
R_EDGE = 1.5       # fillet on all other outer edges

# small hex cavity (2 rows x 3 columns of hexes + central band)
R_HEX = 14.7                       # circumradius of small hex (25.4 A/F)
H_HEX = R_HEX * math.sqrt(3) / 2   # half across-flats
C1_FROM_LEFT = 20.05               # first column centre from left face
N_COL = 3
BAND_HALF = 16.2                   # half height of central band
DEPTH_SMALL = 80.0                 # depth of small cavity

# big hex pocket
R_BIG = 27.9                       # circumradius of big hex
CB_FROM_LEFT = 114.35              # centre from left face
R_BIG_FILLET = 5.0                 # fillet on the four slanted-side corners
R_BIG_TIP_FILLET = 6.0             # fillet on the outer (+X) tip
DEPTH_BIG = 85.0

# side bosses and low pins (both X faces)
BOSS_Y_FROM_FRONT = 30.0
BOSS_R = 12.1
BOSS_H = 3.5
BOLT_R = 20.2
BUMP_R = 3.0
BUMP_H = 0.8
N_BUMP = 8

VIEW = {"azimuth": 45, "elevation": 26}

x0 = -L / 2.0
yf = -D / 2.0

# ---------------- main block with edge treatment ----------------
def block_with_fillets():
    box = cq.Workplane("XY").box(L, D, H).val()
    # large round on the two long back edges (+Y, +-Z)
    back = [e for e in box.Edges()
            if abs(e.tangentAt(0.5).x) > 0.9 and e.Center().y > 0]
    blk = box.fillet(R_BACK, back)

    # small round on every remaining sharp edge
    def is_sharp(e):
        fs = [f for f in blk.Faces() if any(e.isSame(fe) for fe in f.Edges())]
        if len(fs) != 2:
            return False
        p = e.Center()
        return fs[0].normalAt(p).dot(fs[1].normalAt(p)) < 0.9

    sharp = [e for e in blk.Edges() if is_sharp(e)]
    blk = blk.fillet(R_EDGE, sharp)
    return cq.Workplane("XY").add(blk)


body = block_with_fillets()


def hex_prism(cx, cz, r, depth):
    pts = [(cx + r * math.cos(math.radians(a)), cz + r * math.sin(math.radians(a)))
           for a in range(0, 360, 60)]
    return (cq.Workplane("XZ", origin=(0, yf, 0)).polyline(pts).close()
            .extrude(-depth))


def filleted_polygon_prism(pts_r, depth):
    """pts_r: list of (x, z, r) polygon vertices (CCW) with fillet radius r."""
    n = len(pts_r)
    segs = []
    for i in range(n):
        px, pz, r = pts_r[i]
        ax, az, _ = pts_r[i - 1]
        bx, bz, _ = pts_r[(i + 1) % n]
        if r <= 0:
            segs.append(((px, pz), None, (px, pz)))
            continue
        u1 = (ax - px, az - pz)
        u2 = (bx - px, bz - pz)
        l1 = math.hypot(*u1)
        l2 = math.hypot(*u2)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (u2[0] / l2, u2[1] / l2)
        ang = math.acos(max(-1, min(1, u1[0] * u2[0] + u1[1] * u2[1])))
        t = r / math.tan(ang / 2)
        p1 = (px + u1[0] * t, pz + u1[1] * t)
        p2 = (px + u2[0] * t, pz + u2[1] * t)
        bis = (u1[0] + u2[0], u1[1] + u2[1])
        bl = math.hypot(*bis)
        bis = (bis[0] / bl, bis[1] / bl)
        dc = r / math.sin(ang / 2)
        cx, cz = px + bis[0] * dc, pz + bis[1] * dc
        mid = (cx - bis[0] * r, cz - bis[1] * r)
        segs.append((p1, mid, p2))
    wp = cq.Workplane("XZ", origin=(0, yf, 0)).moveTo(*segs[0][0])
    for i, (p1, mid, p2) in enumerate(segs):
        if i > 0:
            wp = wp.lineTo(*p1)
        if mid is not None:
            wp = wp.threePointArc(mid, p2)
    wp = wp.close()
    return wp.extrude(-depth)


# ---------------- small hex cavity ----------------
c1 = x0 + C1_FROM_LEFT
cb = x0 + CB_FROM_LEFT
small = None
for i in range(N_COL):
    cx = c1 + i * 2 * R_HEX
    for cz in (H_HEX, -H_HEX):
        p = hex_prism(cx, cz, R_HEX, DEPTH_SMALL)
        small = p if small is None else small.union(p)
band = (cq.Workplane("XZ", origin=(0, yf, 0))
        .center((c1 + cb) / 2, 0)
        .rect(cb - c1, 2 * BAND_HALF).extrude(-DEPTH_SMALL))
small = small.union(band)

# ---------------- big hex pocket ----------------
big_pts = []
for a in range(0, 360, 60):
    # inner tip (towards the small cavity) stays sharp
    r = 0.0 if a == 180 else (R_BIG_TIP_FILLET if a == 0 else R_BIG_FILLET)
    big_pts.append((cb + R_BIG * math.cos(math.radians(a)),
                    R_BIG * math.sin(math.radians(a)), r))
big = filleted_polygon_prism(big_pts, DEPTH_BIG)

body = body.cut(small).cut(big)

# ---------------- bosses and pins on both X faces ----------------
by = yf + BOSS_Y_FROM_FRONT
for sgn in (1, -1):
    xf = sgn * L / 2
    wp = cq.Workplane("YZ", origin=(xf, 0, 0))
    boss = wp.center(by, 0).circle(BOSS_R).extrude(sgn * BOSS_H)
    body = body.union(boss)
    for k in range(N_BUMP):
        a = math.radians(90 + k * 360.0 / N_BUMP)
        yy = by + BOLT_R * math.cos(a)
        zz = BOLT_R * math.sin(a)
        bump = (cq.Workplane("YZ", origin=(xf - sgn * 0.2, 0, 0))
                .center(yy, zz).circle(BUMP_R).extrude(sgn * (BUMP_H + 0.2)))
        body = body.union(bump)

result = body
